import math
import numpy as np
import cadquery as cq
from OCP.BRepOffsetAPI import BRepOffsetAPI_ThruSections
from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeVertex
from OCP.gp import gp_Pnt

# ============ driving dimensions (mm) ============
U = 0.395                    # mm per design unit (overall scale)

# ---- body: egg-shaped blob with squarish cross sections, built in a local
#      frame (local z = body axis) and then tilted back about X ----
BODY_A = 92.70 * U           # half width (X) of the mid section
BODY_B = 92.39 * U           # half depth (local y) of the mid section
BODY_CT = 145.87 * U         # axis length from centre to top pole
BODY_CB = 110.24 * U         # axis length from centre to bottom pole
POLE_TOP = 2.373             # dome exponent toward the top pole
POLE_BOT = 2.341             # dome exponent toward the bottom pole
WIDTH_KNOTS = (-1.0, -0.6, -0.2, 0.2, 0.6, 1.0)
WIDTH_PROFILE = (1.2881, 1.2534, 1.071, 1.0, 0.9723, 0.8583)   # width factor along the axis
DEPTH_PROFILE = (0.9285, 1.0, 0.8838)                       # depth factor at t=-1,0,1
AXIS_SHIFT = 1.794 * U      # section centres drift toward the back with height
SQUARE_Q0 = 2.3671           # super-ellipse exponent at mid height
SQUARE_Q1 = 0.2969           # change of exponent from bottom to top
FRONT_BACK_DEPTH = 0.0890    # front half deeper than back half (fraction)
FRONT_BACK_SQUARE = 0.5157   # front half squarer than back half
TILT = 35.84                 # body axis leans back (toward +Y), degrees
STATIONS = (-0.97, -0.85, -0.6, -0.3, 0.0, 0.3, 0.6, 0.85, 0.97)
SPLIT_Z = 0.0                # waist plane splitting the skin into two panels

# ---- fins (positions relative to the body's bounding-box centre) ----
# big rear fins: point backward (+Y) low on the body, one each side
BIG_FIN_BASE = (57.0 * U, 14.0 * U, -95.5 * U)    # root bulb centre (in the body)
BIG_FIN_TIP = (70.0 * U, 92.3 * U, -96.5 * U)     # extreme tip point
BIG_FIN_R_ROOT = 16.5 * U
BIG_FIN_ROOT_LEN = 0.25                          # fraction of length kept near root radius
BIG_FIN_R_TIP = 5.0 * U
BIG_FIN_TAPER = 15.0                             # flank half angle near the tip (deg)
# small fins: hang down (-Z) at the back, one each side
SMALL_FIN_BASE = (60.0 * U, 63.0 * U, -34.0 * U)
SMALL_FIN_TIP = (64.0 * U, 76.0 * U, -77.1 * U)
SMALL_FIN_R_ROOT = 11.0 * U
SMALL_FIN_ROOT_LEN = 0.15
SMALL_FIN_R_TIP = 3.6 * U
SMALL_FIN_TAPER = 16.0
FIN_ROOT_FILLET = 6.5 * U                        # blend radius where fins meet the body

# ---- shallow recessed details; recess floors follow the skin ----
RECESS_SCALE = 0.978                             # floor = skin scaled toward the centre
MOUTH_CENTER = (0.0, -74.0 * U, 53.0 * U)         # wide slot on the front-top face
MOUTH_NORMAL = (0.0, -0.77, 0.64)
MOUTH_LENGTH = 95.0 * U
MOUTH_WIDTH = 16.0 * U
EYE_CENTER = (35.0 * U, 103.0 * U, 40.0 * U)      # oval eyes on the back, mirrored in X
EYE_NORMAL = (0.28, 0.96, 0.0)
EYE_LENGTH = 14.0 * U
EYE_WIDTH = 7.5 * U
SMILE_CENTER = (0.0, 102.0 * U, 13.0 * U)         # lens-shaped slit below the eyes
SMILE_NORMAL = (0.0, 0.94, -0.33)
SMILE_LENGTH = 76.0 * U
SMILE_HEIGHT = 17.0 * U

VIEW = {"azimuth": 45, "elevation": 26}


def _interp(knots, vals, t):
    return float(np.polyval(np.polyfit(knots, vals, len(knots) - 1), t))


def _natural_spline(knots, vals, t):
    """Natural cubic spline through (knots, vals) evaluated at t."""
    x = np.asarray(knots, float)
    y = np.asarray(vals, float)
    n = len(x)
    h = np.diff(x)
    m = np.zeros((n, n))
    r = np.zeros(n)
    m[0, 0] = m[-1, -1] = 1.0
    for i in range(1, n - 1):
        m[i, i - 1], m[i, i], m[i, i + 1] = h[i - 1], 2 * (h[i - 1] + h[i]), h[i]
        r[i] = 6 * ((y[i + 1] - y[i]) / h[i] - (y[i] - y[i - 1]) / h[i - 1])
    mm = np.linalg.solve(m, r)
    k = min(max(int(np.searchsorted(x, t) - 1), 0), n - 2)
    a, b = x[k + 1] - t, t - x[k]
    return float((mm[k] * a ** 3 + mm[k + 1] * b ** 3) / (6 * h[k])
                 + (y[k] / h[k] - mm[k] * h[k] / 6) * a
                 + (y[k + 1] / h[k] - mm[k + 1] * h[k] / 6) * b)


def body_section(t):
    pz = POLE_TOP if t > 0 else POLE_BOT
    e = max(1.0 - abs(t) ** pz, 0.0) ** (1.0 / pz)
    a = BODY_A * e * _natural_spline(WIDTH_KNOTS, WIDTH_PROFILE, t)
    b = BODY_B * e * _interp([-1, 0, 1], DEPTH_PROFILE, t)
    z = BODY_CT * t if t > 0 else BODY_CB * t
    yo = AXIS_SHIFT * t
    q = SQUARE_Q0 + SQUARE_Q1 * t
    return a, b, z, yo, q


def section_wire(t, n=16):
    a, b, z, yo, q = body_section(t)
    pts = []
    for i in range(n):
        th = 2.0 * math.pi * (i + 0.5) / n + math.pi / 2
        c, s = math.cos(th), math.sin(th)
        if s < 0:
            bb, qy = b * (1 + FRONT_BACK_DEPTH), q + FRONT_BACK_SQUARE
        else:
            bb, qy = b * (1 - FRONT_BACK_DEPTH), q - FRONT_BACK_SQUARE
        x = a * math.copysign(abs(c) ** (2.0 / q), c)
        y = yo + bb * math.copysign(abs(s) ** (2.0 / qy), s)
        pts.append(cq.Vector(x, y, z))
    return cq.Wire.assembleEdges([cq.Edge.makeSpline(pts, periodic=True)])


def make_body():
    loft = BRepOffsetAPI_ThruSections(True, False, 1e-6)
    loft.AddVertex(BRepBuilderAPI_MakeVertex(gp_Pnt(0, -AXIS_SHIFT, -BODY_CB)).Vertex())
    for t in STATIONS:
        loft.AddWire(section_wire(t).wrapped)
    loft.AddVertex(BRepBuilderAPI_MakeVertex(gp_Pnt(0, AXIS_SHIFT, BODY_CT)).Vertex())
    loft.Build()
    solid = cq.Solid(loft.Shape())
    # split the skin at the waist plane into a lower and an upper panel
    # (same surface, so the skin stays smooth) and rejoin them
    halves = cq.Workplane("XY").add(solid).split(
        cq.Workplane("XY").add(cq.Face.makePlane(1000, 1000, cq.Vector(0, 0, SPLIT_Z), cq.Vector(0, 0, 1)))
    ).solids().vals()
    solid = cq.Workplane("XY").add(halves[0]).union(cq.Workplane("XY").add(halves[1]), clean=False).val()
    solid = solid.rotate(cq.Vector(0, 0, 0), cq.Vector(1, 0, 0), -TILT)
    # centre the body on its bounding box
    verts, _ = solid.tessellate(0.05, 0.1)
    pts = np.array([[v.x, v.y, v.z] for v in verts])
    ctr = (pts.min(axis=0) + pts.max(axis=0)) / 2.0
    return solid.translate(cq.Vector(*(-ctr)))


def make_fin(base, tip, r_root, root_len, r_tip, taper):
    """Horn-shaped fin revolved about the base->tip axis: a spherical root
    bulb (buried in the body), an ogive flank and a spherical rounded tip."""
    base, tip = cq.Vector(*base), cq.Vector(*tip)
    axis = tip - base
    length = axis.Length
    cz = length - r_tip                       # centre of the tip sphere
    al = math.radians(taper)
    tx, tz = r_tip * math.cos(al), cz + r_tip * math.sin(al)   # flank/tip tangency
    mz = root_len * length
    mid = (al + math.pi / 2) / 2
    r45 = r_root * math.sqrt(0.5)
    prof = (
        cq.Workplane("XZ")
        .moveTo(0, -r_root)
        .threePointArc((r45, -r45), (r_root, 0))
        .spline([(r_root * 0.985, mz), (tx, tz)],
                tangents=[(0, 1), (0, 1), (-math.sin(al), math.cos(al))],
                includeCurrent=True)
        .threePointArc((r_tip * math.cos(mid), cz + r_tip * math.sin(mid)), (0, length))
        .close()
    )
    fin = prof.revolve(360, (0, 0, 0), (0, 1, 0)).val()
    # the XZ workplane maps local y to global Z; fin axis is now global +Z
    zdir = cq.Vector(0, 0, 1)
    ax = axis.normalized()
    rot_axis = zdir.cross(ax)
    if rot_axis.Length > 1e-9:
        ang = math.degrees(math.acos(max(-1.0, min(1.0, zdir.dot(ax)))))
        fin = fin.rotate(cq.Vector(0, 0, 0), rot_axis, ang)
    return fin.translate(base)


def mirror_x(p):
    return (-p[0], p[1], p[2])


body = make_body()
big = (BIG_FIN_R_ROOT, BIG_FIN_ROOT_LEN, BIG_FIN_R_TIP, BIG_FIN_TAPER)
small = (SMALL_FIN_R_ROOT, SMALL_FIN_ROOT_LEN, SMALL_FIN_R_TIP, SMALL_FIN_TAPER)
fins = [
    make_fin(BIG_FIN_BASE, BIG_FIN_TIP, *big),
    make_fin(mirror_x(BIG_FIN_BASE), mirror_x(BIG_FIN_TIP), *big),
    make_fin(SMALL_FIN_BASE, SMALL_FIN_TIP, *small),
    make_fin(mirror_x(SMALL_FIN_BASE), mirror_x(SMALL_FIN_TIP), *small),
]

part = cq.Workplane("XY").add(body)
for f in fins:
    part = part.union(cq.Workplane("XY").add(f), clean=False)


def root_edges(shape):
    """Edges where a fin meets the body skin."""
    out = []
    for e in shape.Edges():
        p = e.positionAt(0.5)
        v = cq.Vertex.makeVertex(p.x, p.y, p.z)
        if body.distance(v) < 1e-3 and min(f.distance(v) for f in fins) < 1e-3:
            out.append(e)
    return out


shape = part.val()
shape = shape.fillet(FIN_ROOT_FILLET, root_edges(shape))

def recess_tool(center, normal, sketch):
    """Prism through the skin along -normal carrying the given 2D outline."""
    n = cq.Vector(*normal).normalized()
    c = cq.Vector(*center)
    xdir = cq.Vector(1, 0, 0)
    xdir = (xdir - n * xdir.dot(n)).normalized()
    plane = cq.Plane(origin=c + n * (15 * U), xDir=xdir, normal=-n)
    return sketch(cq.Workplane(plane)).extrude(30 * U).val()


def lens(wp, length, height):
    return (wp.moveTo(-length / 2, 0)
            .threePointArc((0, height / 2), (length / 2, 0))
            .threePointArc((0, -height / 2), (-length / 2, 0))
            .close())


tools = [
    recess_tool(MOUTH_CENTER, MOUTH_NORMAL, lambda wp: wp.slot2D(MOUTH_LENGTH, MOUTH_WIDTH)),
    recess_tool(EYE_CENTER, EYE_NORMAL, lambda wp: wp.ellipse(EYE_LENGTH / 2, EYE_WIDTH / 2)),
    recess_tool(mirror_x(EYE_CENTER), mirror_x(EYE_NORMAL), lambda wp: wp.ellipse(EYE_LENGTH / 2, EYE_WIDTH / 2)),
    recess_tool(SMILE_CENTER, SMILE_NORMAL, lambda wp: lens(wp, SMILE_LENGTH, SMILE_HEIGHT)),
]
floor = body.scale(RECESS_SCALE)
for tool in tools:
    shape = shape.cut(tool.cut(floor))

result = cq.Workplane("XY").add(shape)
